import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H_BACK = 236.0      # blade height at the back edge (+Y), inner face peak
H_FRONT = 195.0     # blade height at the front edge (-Y)
DEPTH = 46.6        # blade depth along Y
THK = 5.3           # blade thickness along X
BEVEL_W = 15.5      # width of the front-edge bevel on the outer face (at the bottom)
BEVEL_W_TOP = 13.0  # bevel boundary position at the top of the bevel (from the bottom knife)
TOP_BEV_Z = 187.0   # height where the top bevel meets the front bevel (outer face)
PEAK_DROP = 1.0     # outer face back-top corner sits this much below the peak
SPACING = 31.5      # centre distance between the two blades (X)
Y_SHIFT = 4.1       # right blade is shifted +Y relative to the left one
LEAN = 2.3          # knife front edge leans back by this much at its top
SPLAY_DEG = 1.1     # each blade is turned so its front opens outward

# bracket plate on the outer face (blade-local Y, Z)
BR_Y0, BR_Y1 = -7.0, 9.0
BR_H = 30.8
BR_T = 1.8
HOLE_D = 2.8
CSK_D = 4.6
HOLE_Z = (8.6, 21.0)

# engraved decoration
GROOVE_W = 0.7
GROOVE_D = 0.6
POCKET_D = 1.0

# pin
PIN_X, PIN_Y = -70.0, -55.7
PIN_BASE_D, PIN_BASE_H = 11.6, 1.1
PIN_SHAFT_D = 7.4
PIN_COLLAR_D, PIN_COLLAR_H = 10.2, 4.5
PIN_TOP_D, PIN_TOP_H = 7.4, 2.8
PIN_LEN = 54.5

# small dowel lying along Y
DOW_X, DOW_Y, DOW_Z = -88.6, 24.3, 5.0
DOW_D, DOW_L = 1.3, 2.3


def poly_wire(x, pts):
    return cq.Wire.makePolygon([cq.Vector(x, y, z) for y, z in pts], close=True)


def poly_pocket(x0, depth, pts):
    """Prism from a (Y,Z) polygon starting at X=x0 going -X by depth."""
    f = cq.Face.makeFromWires(poly_wire(x0, pts))
    return cq.Solid.extrudeLinear(f, cq.Vector(-depth, 0, 0))


def groove_ring(x0, depth, pts, width):
    """Closed outline groove following a (Y,Z) polygon."""
    w = poly_wire(x0, pts)
    wi = w.offset2D(-width, "intersection")[0]
    so = cq.Solid.extrudeLinear(cq.Face.makeFromWires(w), cq.Vector(-depth, 0, 0))
    si = cq.Solid.extrudeLinear(cq.Face.makeFromWires(wi), cq.Vector(-depth, 0, 0))
    return so.cut(si)


def line_groove(x0, depth, a, b, width):
    """Straight round-ended groove from a to b (Y,Z) cut into the face X=x0."""
    (ya, za), (yb, zb) = a, b
    L = math.hypot(yb - ya, zb - za)
    ang = math.degrees(math.atan2(zb - za, yb - ya))
    return (
        cq.Workplane("YZ", origin=(x0 - depth, 0, 0))
        .center((ya + yb) / 2, (za + zb) / 2)
        .transformed(rotate=(0, 0, ang))
        .slot2D(L + width, width)
        .extrude(depth + 0.5)
        .val()
    )


def make_blade():
    """Right-hand blade: flat inner face at X=-THK/2, bevelled outer face at X=+THK/2.

    Built as a ruled loft between the inner-face outline (knife edges along the
    front and along the slanted top) and the outer-face outline, which is set
    back by the front bevel and by a top bevel that widens toward the front.
    """
    xi, xo = -THK / 2.0, THK / 2.0
    d2 = DEPTH / 2.0
    inner = [(-d2, 0.0), (d2, 0.0), (d2, H_BACK), (-d2 + LEAN, H_FRONT)]
    outer = [(-d2 + BEVEL_W, 0.0), (d2, 0.0), (d2, H_BACK - PEAK_DROP),
             (-d2 + BEVEL_W_TOP, TOP_BEV_Z)]
    blade = cq.Workplane().add(
        cq.Solid.makeLoft([poly_wire(xi, inner), poly_wire(xo, outer)], ruled=True)
    )

    # bracket plate with two countersunk through holes
    yc = (BR_Y0 + BR_Y1) / 2
    plate = (
        cq.Workplane("YZ", origin=(xo - 0.01, 0, 0))
        .center(yc, BR_H / 2)
        .rect(BR_Y1 - BR_Y0, BR_H)
        .extrude(BR_T + 0.01)
    )
    blade = blade.union(plate)
    top_x = xo + BR_T
    for hz in HOLE_Z:
        h = (
            cq.Workplane("YZ", origin=(xi - 1, 0, 0))
            .center(yc, hz)
            .circle(HOLE_D / 2)
            .extrude(THK + BR_T + 2)
        )
        blade = blade.cut(h)
        r1 = CSK_D / 2
        cone = cq.Solid.makeCone(r1, 0.0, r1, cq.Vector(top_x, yc, hz), cq.Vector(-1, 0, 0))
        blade = blade.cut(cq.Workplane().add(cone))

    # engraved decoration on the outer face
    xs = xo + 0.01
    cuts = []
    band = [(-4.8, 73.5), (0.1, 73.5), (14.6, 62.6), (16.0, 58.6), (d2 + 2.0, 50.3),
            (d2 + 2.0, 36.7), (18.3, 42.2), (8.8, 49.0), (8.3, 52.0), (-2.1, 59.8),
            (-2.1, 65.4), (-5.6, 68.3)]
    cuts.append(groove_ring(xs, GROOVE_D, band, GROOVE_W))

    lines = [
        ((-5.3, 46.9), (12.1, 36.1)),
        ((12.1, 36.1), (13.1, 31.1)),
        ((13.1, 31.1), (22.9, 22.9)),
        ((-5.3, 38.9), (6.6, 31.3)),
        ((12.6, 28.0), (22.8, 21.0)),
        ((12.2, 7.3), (23.0, 2.9)),
    ]
    for a, b in lines:
        cuts.append(line_groove(xs, GROOVE_D, a, b, GROOVE_W))

    # hexagonal pocket and small notch right of the bracket
    hexa = [(11.7, 21.4), (14.5, 21.1), (21.1, 15.7), (21.4, 11.3), (17.6, 10.8), (11.4, 15.4)]
    cuts.append(poly_pocket(xs, POCKET_D, hexa))
    notch = [(14.5, 10.3), (20.2, 8.4), (21.4, 5.8), (19.0, 7.2)]
    cuts.append(poly_pocket(xs, GROOVE_D, notch))

    # vertical comb slots below the band
    for i in range(3):
        cuts.append(
            cq.Workplane("YZ", origin=(xs - GROOVE_D, 0, 0))
            .center(16.6 + 1.5 * i, 37.8 - 0.6 * i)
            .rect(0.7, 8.5)
            .extrude(GROOVE_D + 0.5)
            .val()
        )
    for c in cuts:
        blade = blade.cut(cq.Workplane().add(c))
    # splay: pivot about the vertical back edge of the inner face
    blade = blade.rotate((xi, d2, 0), (xi, d2, 1), SPLAY_DEG)
    return blade


blade_r = make_blade()
blade_l = blade_r.mirror("YZ")

blade_r = blade_r.translate((SPACING / 2, Y_SHIFT / 2, 0))
blade_l = blade_l.translate((-SPACING / 2, -Y_SHIFT / 2, 0))

# ---------------- pin ----------------
shaft_top = PIN_LEN - PIN_TOP_H - PIN_COLLAR_H
pin = (
    cq.Workplane("XY")
    .circle(PIN_BASE_D / 2).extrude(PIN_BASE_H)
    .edges(">Z").fillet(0.4)
    .faces(">Z").workplane().circle(PIN_SHAFT_D / 2).extrude(shaft_top - PIN_BASE_H)
)
collar = (
    cq.Workplane("XY", origin=(0, 0, shaft_top))
    .circle(PIN_COLLAR_D / 2).extrude(PIN_COLLAR_H)
    .edges().fillet(0.5)
)
top = (
    cq.Workplane("XY", origin=(0, 0, shaft_top + PIN_COLLAR_H))
    .circle(PIN_TOP_D / 2).extrude(PIN_TOP_H)
    .faces(">Z").edges().fillet(0.6)
)
pin = pin.union(collar).union(top).translate((PIN_X, PIN_Y, 0))

# ---------------- small dowel ----------------
dowel = (
    cq.Workplane("XZ", origin=(DOW_X, DOW_Y + DOW_L / 2, DOW_Z))
    .circle(DOW_D / 2)
    .extrude(DOW_L)
)

result = blade_r.union(blade_l).union(pin).union(dowel)
